import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
W = 100.0              # plate width (flat-to-flat across X and Y)
HALF = W / 2
CH = 12.2              # plate corner chamfer leg
SAG = 9.2              # sagitta of the concave side arcs
T_PLATE = 3.2          # plate thickness
H_FLARE = 8.3          # height of the flared body under the plate
H_DISC = 3.7           # height of the scalloped disc
R_DISC = 36.6          # disc radius
N_SCAL = 21            # number of scallops round the disc
R_SCAL = 5.1           # scallop radius (centres on the disc rim, narrow lands between)

# main flare: revolved cove, tangent to plate underside
FL_R_TAN = 54.5        # radius where cove meets plate underside
FL_COVE = 21.3         # cove radius
# +X side lobe (lofted through three sections)
LOBE_R_BOT = 37.7     # radius at flare bottom
LOBE_D_MID = 3.0       # depth of middle section below plate
LOBE_X_MID = 39.6      # x of middle section on the X axis
LOBE_T_MID = 46.5      # distance of middle-section corners along the diagonal
LOBE_IN = (16.0, 6.0)  # inner (hidden) corner of the loft sections
# corner ribs (diagonal gussets) under the chamfered corners
G_R_TAN = 62.4         # rib cove meets the plate at the chamfer
G_BOT = 38.0           # rib underside ends on the flare-foot circle
G_HALF_W = CH / math.sqrt(2) + 0.4  # half width ~ half chamfer length (slightly wider)

# holes in the +Y side face
N_HOLES = 7
HOLE_PITCH = 11.3
HOLE_D = 1.3
HOLE_DEPTH = 4.0

Z_DISC_TOP = H_DISC
Z_PLATE_BOT = H_DISC + H_FLARE
Z_TOP = Z_PLATE_BOT + T_PLATE
R_HOLLOW = 15.0        # flare rings are hollow at the axis (filled by a core)


def outline(wp):
    a = HALF
    c = a - CH
    s = SAG
    return (wp.moveTo(-c, -a)
              .threePointArc((0, -a + s), (c, -a))
              .lineTo(a, -c)
              .threePointArc((a - s, 0), (a, c))
              .lineTo(c, a)
              .threePointArc((0, a - s), (-c, a))
              .lineTo(-a, c)
              .threePointArc((-a + s, 0), (-a, -c))
              .close())


def cove_pt(r_tan, rad, d):
    """point on a cove arc tangent to plate underside at r_tan, depth d below plate"""
    return (r_tan - math.sqrt(rad ** 2 - (rad - d) ** 2), Z_PLATE_BOT - d)


# ---------------- plate ----------------
plate = outline(cq.Workplane("XY").workplane(offset=Z_PLATE_BOT)).extrude(T_PLATE)

# ---------------- main revolved flare (ring) ----------------
p_bot = cove_pt(FL_R_TAN, FL_COVE, H_FLARE)
p_mid = cove_pt(FL_R_TAN, FL_COVE, H_FLARE * 0.4)
ringF = (cq.Workplane("XZ")
         .moveTo(R_HOLLOW, Z_DISC_TOP)
         .lineTo(*p_bot)
         .threePointArc(p_mid, (FL_R_TAN, Z_PLATE_BOT))
         .lineTo(R_HOLLOW, Z_PLATE_BOT)
         .close()
         .revolve(360, (0, 0, 0), (0, 1, 0)))

# ---------------- +X side: smooth lofted lobe ----------------
# On the +X side the body is a lofted surface running from the plate's +X
# side arc down to the flare circle, bounded by the two corner ribs.
R_ARC = ((HALF - CH) ** 2 + SAG ** 2) / (2 * SAG)
wedge = (cq.Workplane("XY").workplane(offset=Z_DISC_TOP - 1)
         .polyline([(0, 0), (90, 90), (90, -90)]).close()
         .extrude(H_FLARE + 2))
core = (cq.Workplane("XY").workplane(offset=Z_DISC_TOP)
        .circle(R_HOLLOW + 5).extrude(H_FLARE))


def rib_edge_pt(t, sgn):
    """point just inside the +X-facing side plane of a corner rib at distance t"""
    s = CH / math.sqrt(2)
    return ((t + s) / math.sqrt(2), sgn * (t - s) / math.sqrt(2))


def lobe_section(wp, pa, mid, pb):
    return (wp.moveTo(LOBE_IN[0], -LOBE_IN[1]).lineTo(*pa)
              .threePointArc(mid, pb).lineTo(LOBE_IN[0], LOBE_IN[1]).close())


# bottom section: flare circle between the rib side planes
qx = CH / 2
qy = math.sqrt(LOBE_R_BOT ** 2 / 2 - qx ** 2 + 1e-9)
pa0 = (qx + qy, -(qy - qx))
pb0 = (qx + qy, (qy - qx))
pa1 = rib_edge_pt(LOBE_T_MID, -1)
pb1 = rib_edge_pt(LOBE_T_MID, 1)
pa2 = (HALF, -(HALF - CH))
pb2 = (HALF, HALF - CH)
wp0 = cq.Workplane("XY").workplane(offset=Z_DISC_TOP)
lobe = lobe_section(wp0, pa0, (LOBE_R_BOT, 0), pb0)
lobe = lobe_section(lobe.workplane(offset=H_FLARE - LOBE_D_MID), pa1, (LOBE_X_MID, 0), pb1)
lobe = lobe_section(lobe.workplane(offset=LOBE_D_MID), pa2, (HALF - SAG, 0), pb2)
lobe = lobe.loft(ruled=False, combine=True)

flare = ringF.cut(wedge).union(core).union(lobe)

# ---------------- corner gussets ----------------
# the ribs' underside is a circular cove revolved about Z (so the rib ends on
# the flare-foot circle); its crest lies just outboard of the chamfer so the
# cove leaves the plate underside at a small positive angle
g_cx = G_R_TAN + 2.0
g_cz = (((G_BOT - g_cx) ** 2 + Z_DISC_TOP ** 2 - (G_R_TAN - g_cx) ** 2 - Z_PLATE_BOT ** 2)
        / (2 * (Z_DISC_TOP - Z_PLATE_BOT)))
g_rad = math.hypot(G_R_TAN - g_cx, Z_PLATE_BOT - g_cz)
g_zm = Z_PLATE_BOT - 0.4 * H_FLARE
g_mid = (g_cx - math.sqrt(g_rad ** 2 - (g_zm - g_cz) ** 2), g_zm)
ringG = (cq.Workplane("XZ")
         .moveTo(R_HOLLOW, Z_DISC_TOP)
         .lineTo(G_BOT, Z_DISC_TOP)
         .threePointArc(g_mid, (G_R_TAN, Z_PLATE_BOT))
         .lineTo(R_HOLLOW, Z_PLATE_BOT)
         .close()
         .revolve(360, (0, 0, 0), (0, 1, 0)))
slabs = None
for ang in (45, -45):
    sl = (cq.Workplane("XY").workplane(offset=Z_DISC_TOP - 1)
          .rect(2 * (HALF + 25), 2 * G_HALF_W).extrude(H_FLARE + 2)
          .rotate((0, 0, 0), (0, 0, 1), ang))
    slabs = sl if slabs is None else slabs.union(sl)
gussets = ringG.intersect(slabs)
body = flare.union(gussets)

prism = outline(cq.Workplane("XY").workplane(offset=Z_DISC_TOP - 1)).extrude(H_FLARE + 2)
body = body.intersect(prism)

# ---------------- scalloped disc ----------------
disc = cq.Workplane("XY").circle(R_DISC).extrude(H_DISC)
cutters = None
for i in range(N_SCAL):
    ang = math.radians(-90 + i * 360.0 / N_SCAL)
    cx, cy = R_DISC * math.cos(ang), R_DISC * math.sin(ang)
    c_ = (cq.Workplane("XY").workplane(offset=-1)
          .center(cx, cy).circle(R_SCAL).extrude(H_DISC + 2))
    cutters = c_ if cutters is None else cutters.union(c_)
disc = disc.cut(cutters)

result = plate.union(body).union(disc)

# ---------------- small holes in the +Y side face ----------------
for k in range(N_HOLES):
    x = (k - (N_HOLES - 1) / 2) * HOLE_PITCH
    y_face = (HALF - SAG + R_ARC) - math.sqrt(R_ARC ** 2 - x ** 2)
    hole = (cq.Workplane("XZ", origin=(0, y_face + 2, 0))
            .center(x, Z_PLATE_BOT + T_PLATE / 2)
            .circle(HOLE_D / 2).extrude(HOLE_DEPTH + 2))
    result = result.cut(hole)
